import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
U = 19.0                  # key pitch
LAYOUT_DX = 0.25          # layout offset from plate centre (X)
PLATE_W = 285.0           # plate width  (X)
PLATE_H = 94.6            # plate depth  (Y)
PLATE_T = 1.5             # plate thickness (Z)
CORNER_R = 2.0            # plate corner radius

SW = 14.0                 # switch cutout square
NOTCH_W = 0.8             # side opening notch depth
NOTCH_Y0 = 2.9            # notch from y=+-2.9 ...
NOTCH_Y1 = 6.0            # ... to y=+-6.0

# Cherry stabiliser cutout (relative to stab centre)
STAB_HW = 3.325           # half width of housing cutout
STAB_TOP = 5.53
STAB_BOT = -6.77
STAB_TAB_HW = 1.65        # bottom tab half width
STAB_TAB_BOT = -7.97
STAB_SIDE_W = 0.875       # outward side notch
STAB_SIDE_Y0 = -0.5
STAB_SIDE_Y1 = 2.3
COSTAR_HW = 1.65          # costar insert slot half width
COSTAR_HH = 7.0           # costar insert slot half height (centred on housing)
STAB_2U = 11.938          # stab offset for 2u..2.75u
SPACE_STABS = (40.0, 50.0)  # spacebar stab offsets
SPACE_SLOT_H = 4.5        # slot joining spacebar switch and stabs

HOLE_D = 2.9
# holes, measured from plate top-left corner (x right, y down)
HOLES = [(25.2, 27.8), (128.0, 48.2), (190.2, 84.9),
         (259.4, 27.7), (4.9, 56.1), (279.4, 56.1)]

# ---------------- layout (ANSI 60%) ----------------
# rows: list of (width_in_u) ; row 0 is the number row (back, +Y)
ROWS = [
    [1] * 13 + [2],
    [1.5] + [1] * 12 + [1.5],
    [1.75] + [1] * 11 + [2.25],
    [2.25] + [1] * 10 + [2.75],
    [1.25] * 3 + [6.25] + [1.25] * 4,
]
LAYOUT_W = 15 * U
LAYOUT_H = 5 * U


def rects_for_key(cx, cy, w):
    """Return list of (x, y, w, h) rectangles forming one key cutout."""
    r = []
    # switch cutout with side openings
    r.append((cx, cy, SW, SW))
    ny = (NOTCH_Y0 + NOTCH_Y1) / 2.0
    nh = NOTCH_Y1 - NOTCH_Y0
    for sy in (1, -1):
        r.append((cx, cy + sy * ny, SW + 2 * NOTCH_W, nh))

    def stab(sx, outward):
        # main housing
        r.append((sx, cy + (STAB_TOP + STAB_BOT) / 2, 2 * STAB_HW, STAB_TOP - STAB_BOT))
        # costar insert slot
        r.append((sx, cy + (STAB_TOP + STAB_BOT) / 2, 2 * COSTAR_HW, 2 * COSTAR_HH))
        # bottom tab
        r.append((sx, cy + (STAB_BOT + STAB_TAB_BOT) / 2, 2 * STAB_TAB_HW, STAB_BOT - STAB_TAB_BOT))
        # outward side notch
        r.append((sx + outward * (STAB_HW + STAB_SIDE_W / 2), cy + (STAB_SIDE_Y0 + STAB_SIDE_Y1) / 2,
                  STAB_SIDE_W, STAB_SIDE_Y1 - STAB_SIDE_Y0))

    if 2 <= w < 3:
        for sgn in (1, -1):
            stab(cx + sgn * STAB_2U, sgn)
        # bridge between switch and stabs
        span = 2 * (STAB_2U - STAB_HW) + 0.01
        r.append((cx, cy + (STAB_TOP + STAB_BOT) / 2, span, STAB_TOP - STAB_BOT))
    elif w >= 6:
        for sgn in (1, -1):
            for off in SPACE_STABS:
                stab(cx + sgn * off, sgn)
        far = max(SPACE_STABS)
        r.append((cx, cy, 2 * far, SPACE_SLOT_H))
    return r


sk = cq.Sketch().rect(PLATE_W, PLATE_H).vertices().fillet(CORNER_R)

cut_rects = []
for ri, row in enumerate(ROWS):
    cy = LAYOUT_H / 2 - (ri + 0.5) * U
    xu = 0.0
    for w in row:
        cx = (xu + w / 2) * U - LAYOUT_W / 2 + LAYOUT_DX
        cut_rects += rects_for_key(cx, cy, w)
        xu += w

for (x, y, w, h) in cut_rects:
    sk = sk.push([(x, y)]).rect(w, h, mode="s").reset()

for (hx, hy) in HOLES:
    sk = sk.push([(hx - PLATE_W / 2, PLATE_H / 2 - hy)]).circle(HOLE_D / 2, mode="s").reset()

result = cq.Workplane("XY").placeSketch(sk).extrude(PLATE_T)

VIEW = {"azimuth": 45, "elevation": 26}
